import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_MakePipeShell
from OCP.gp import gp_Ax2, gp_Pnt, gp_Dir

# Aerodynamic hood / fairing: a central hood whose front is a curved ramp
# running out to a knife-edge tip, two side wings with an elliptic round and
# a sloped front cap, and a short rear extension with rounded top edges.
# Moulded as a thick-walled shell, open at the bottom.
# X across, Y front(-) to back(+), Z up; the part sits on Z = 0.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 475.0            # overall length (Y); ramp tip at -L/2 (front)
W_C = 351.0          # width of the central hood (X)
WING_EXT_R = 56.6    # +X wing reach beyond the hood side wall
WING_EXT_L = 62.0    # -X wing reach beyond the hood side wall
H = 56.4             # overall height
T = 8.0              # wall thickness (shell, open bottom)

WING_Y0 = -148.0     # wing front (foot of the cap) Y
WING_Y1 = 143.4      # wing back face Y
WING_A = 49.0        # wing elliptic round: horizontal semi-axis (vertical = H)
REAR_R = 20.0        # top side round of the rear extension

# ramp profile: (distance from tip, height); the last point starts the flat top
RAMP_PTS = [(0.0, 0.0), (26.2, 16.6), (57.0, 30.4), (88.0, 39.6), (110.0, 44.6),
            (130.0, 48.4), (161.0, 52.4), (192.0, 54.6), (232.0, H)]
RAMP_T0 = (1.0, 0.68)               # tangent at the knife-edge tip
RAMP_BREAK = 5                      # point where the wing path rejoins the ramp
WING_DROP = {2: 8.5, 3: 8.5, 4: 6.5}    # wing path dip below the ramp (mm)
WING_KINK = 6.0                     # deg, wing path meets the ramp slightly steeper

# wing front cap (cylinder, axis along X): circle centre (y from WING_Y0, z), radius
CAP_CY, CAP_CZ, CAP_R = 110.2, -38.0, 116.6

# holes
WING_HOLE_D = 13.0                  # vertical holes through the wing rounds
WING_HOLE_X = 206.6
WING_HOLE_Y = (110.6, -115.2)
BACK_HOLE_D = 11.0                  # horizontal holes through the back wall
BACK_HOLE_X = 64.0
BACK_HOLE_Z = 35.6

Y_TIP = -L / 2.0
Y_BACK = L / 2.0
XC = W_C / 2.0
X_MAX = XC + max(WING_EXT_R, WING_EXT_L)
Z_BOT_IN = -12.0                    # cavity body runs out below the floor


# ---------------- ramp curve (and its inward offsets) ----------------
def _ramp_table():
    """Ramp points incl. a run-out beyond the back, with a tangent at every point."""
    pts = RAMP_PTS + [(L + 60.0, H)]
    n = len(pts)
    tans = []
    for i, (s, z) in enumerate(pts):
        if i == 0:
            t = RAMP_T0
        elif i >= n - 2:
            t = (1.0, 0.0)
        else:
            (s0, z0), (s1, z1) = pts[i - 1], pts[i + 1]
            t = (s1 - s0, z1 - z0)
        ln = math.hypot(*t)
        tans.append((t[0] / ln, t[1] / ln))
    return pts, tans


def ramp_points(off):
    """(y, z) ramp points shifted `off` along the inward normal, and tangents."""
    pts, tans = _ramp_table()
    out = [(Y_TIP + s + off * tz, z - off * ty) for (s, z), (ty, tz) in zip(pts, tans)]
    return out, tans


def _spline(x, yz, tans):
    return cq.Edge.makeSpline([cq.Vector(x, y, z) for (y, z) in yz],
                              tangents=[cq.Vector(0, ty, tz) for (ty, tz) in tans])


def ramp_edge(x, off=0.0):
    p, t = ramp_points(off)
    return _spline(x, p, t)


def wing_path_edges(x, off=0.0):
    """Wing section path: dips below the ramp ahead of RAMP_BREAK, then runs
    exactly on the ramp curve (trimmed copy of the same spline)."""
    p, t = ramp_points(off)
    i0, ib = min(WING_DROP), RAMP_BREAK
    fp = [(y, z - WING_DROP.get(i, 0.0)) for i, (y, z) in enumerate(p)][i0:ib + 1]
    a = math.atan2(t[ib][1], t[ib][0]) + math.radians(WING_KINK)
    ft = t[i0:ib] + [(math.cos(a), math.sin(a))]
    front = _spline(x, fp, ft)
    full = ramp_edge(x, off)
    u_b = full.paramAt(cq.Vector(x, *p[ib]))
    rear = full.trim(u_b, full.paramAt(1.0))
    return [front, rear]


def ramp_keep(off=0.0):
    """Solid under the ramp + flat top (YZ profile extruded along X)."""
    x0 = -(X_MAX + 40.0)
    p, _ = ramp_points(off)
    (y_t, z_t), (y_e, z_e) = p[0], p[-1]
    k = RAMP_T0[1] / RAMP_T0[0]
    pa = cq.Vector(x0, y_t - 40.0, z_t - 40.0 * k)
    pt = cq.Vector(x0, y_t, z_t)
    pe = cq.Vector(x0, y_e, z_e)
    pd = cq.Vector(x0, y_e, -60.0)
    pf = cq.Vector(x0, y_t - 40.0, -60.0)
    edges = [cq.Edge.makeLine(pa, pt), ramp_edge(x0, off),
             cq.Edge.makeLine(pe, pd), cq.Edge.makeLine(pd, pf),
             cq.Edge.makeLine(pf, pa)]
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Workplane().add(cq.Solid.extrudeLinear(face, cq.Vector(-2 * x0, 0, 0)))


# ---------------- central hood ----------------
def central_body(off, zb):
    xc, zt, r = XC - off, H - off, REAR_R - off
    y0 = Y_TIP - 40.0
    body = (cq.Workplane("XY")
            .box(2 * xc, (Y_BACK - off) - y0, zt - zb, centered=(True, False, False))
            .translate((0, y0, zb))
            .intersect(ramp_keep(off)))
    # rounded top side edges on the rear extension (behind the wings)
    y1 = WING_Y1 - off
    for sx in (1, -1):
        corner = (cq.Workplane("XY")
                  .box(r + 5.0, Y_BACK + 20.0 - y1, r + 5.0, centered=False)
                  .translate((xc - r, y1, zt - r)))
        round_ = cq.Workplane().add(cq.Solid.makeCylinder(
            r, Y_BACK + 40.0 - y1, cq.Vector(xc - r, y1 - 10.0, zt - r), cq.Vector(0, 1, 0)))
        cutter = corner.cut(round_)
        if sx < 0:
            cutter = cutter.mirror("YZ")
        body = body.cut(cutter)
    return body


# ---------------- side wing ----------------
def wing_profile(y0, off, zb, ext, dz):
    """+X wing cross-section (XZ plane at y0), lifted by dz: flat top + elliptic round."""
    xi, xo = XC - off, XC + ext - off
    wp = (cq.Workplane("XZ", origin=(0, y0, 0))
          .moveTo(xi, zb + dz)
          .lineTo(xo, zb + dz))
    if zb < 0:
        wp = wp.lineTo(xo, dz)
    return (wp.ellipseArc(WING_A - off, H - off, 0, 90, startAtCurrent=True)
            .lineTo(xi, H - off + dz)
            .close())


def translational_sweep(profile_wire, path_edges):
    """Sweep keeping the section parallel to itself (pure translation)."""
    ps = BRepOffsetAPI_MakePipeShell(cq.Wire.assembleEdges(path_edges).wrapped)
    ps.SetMode(gp_Ax2(gp_Pnt(0, 0, 0), gp_Dir(0, 0, 1), gp_Dir(1, 0, 0)))
    ps.Add(profile_wire.wrapped, False, False)
    ps.Build()
    ps.MakeSolid()
    return cq.Solid(ps.Shape())


def wing_body(off, zb, ext):
    # the section rides along the ramp curve: the wing top blends into the
    # hood ramp and the whole wing sinks toward its front
    path = wing_path_edges(XC - off, off)
    p0 = path[0].startPoint()
    prof = wing_profile(p0.y, off, zb, ext, dz=p0.z - (H - off)).val()
    body = cq.Workplane().add(translational_sweep(prof, path))
    y1 = WING_Y1 - off
    clip = (cq.Workplane("XY")
            .box(ext + 40.0, y1 - (Y_TIP - 100.0), H + 60.0 - zb, centered=False)
            .translate((XC - off - 20.0, Y_TIP - 100.0, zb)))
    body = body.intersect(clip)
    # front cap: cylindrical face (axis along X) rising from the wing foot
    cyc, rc = WING_Y0 + CAP_CY, CAP_R - off
    z_lo, z_hi = zb - 5.0, H + 10.0
    zm = 0.5 * (z_lo + z_hi)
    yy = [cyc - math.sqrt(rc ** 2 - (z - CAP_CZ) ** 2) for z in (z_lo, zm, z_hi)]
    cap = (cq.Workplane("YZ", origin=(XC - off - 5.0, 0, 0))
           .moveTo(Y_TIP - 80.0, z_lo)
           .lineTo(yy[0], z_lo)
           .threePointArc((yy[1], zm), (yy[2], z_hi))
           .lineTo(Y_TIP - 80.0, z_hi)
           .close()
           .extrude(ext + 30.0))
    return body.cut(cap)


def envelope(off, zb):
    wing_r = wing_body(off, zb, WING_EXT_R)
    wing_l = wing_body(off, zb, WING_EXT_L).mirror("YZ")
    return central_body(off, zb).union(wing_r).union(wing_l)


# ---------------- shell: outer envelope minus inward-offset cavity ----------------
outer = envelope(0.0, 0.0)
cavity = envelope(T, Z_BOT_IN)
part = outer.cut(cavity)

# ---------------- holes ----------------
for sx in (1, -1):
    for hy in WING_HOLE_Y:
        drill = cq.Solid.makeCylinder(WING_HOLE_D / 2.0, H + 40.0,
                                      cq.Vector(sx * WING_HOLE_X, hy, -20.0),
                                      cq.Vector(0, 0, 1))
        part = part.cut(cq.Workplane().add(drill))
    drill = cq.Solid.makeCylinder(BACK_HOLE_D / 2.0, T + 12.0,
                                  cq.Vector(sx * BACK_HOLE_X, Y_BACK - T - 6.0, BACK_HOLE_Z),
                                  cq.Vector(0, 1, 0))
    part = part.cut(cq.Workplane().add(drill))

result = part
